import math
import cadquery as cq

# =====================================================================================
# Motor / bearing carrier plate: flat plate (back face at Y=0, front face toward -Y)
# with a conical raised boss around the bearing bore, an L-shaped arm with a slot,
# 45 deg chamfer around the front perimeter, counterbored clearance holes.
# =====================================================================================

# ---------------------------------------------------------------- parameters (mm)
T = 5.0            # plate thickness (back face at Y=0, front face at Y=-T)
TB = 7.0           # thickness over the raised boss
C1 = 1.8           # 45 deg chamfer on the front perimeter of the plate
YC = -(T - C1)     # plane where the perimeter chamfer starts

# outline (X to the right, Z up)
TOP_C = (0.0, 16.3)        # top lobe / top hole centre
TOP_R = 7.2
MAIN_C = (0.55, 0.3)       # big left lobe arc (concentric with the boss cone)
MAIN_R = 14.85
RU_C = (1.8, 3.9)          # upper right arc
RU_R = 10.75
X_RIGHT = RU_C[0] + RU_R   # straight right edge of the body (tangent to the upper right arc)
X_LEFT = -7.05             # left edge of the lower block
Z_BOT = -23.8              # bottom edge
Z_ARM_TOP = -10.55         # top edge of the arm
ARM_END_X = 23.5           # centre of the arm end radius
ARM_ZC = (Z_BOT + Z_ARM_TOP) / 2.0
ARM_R = (Z_ARM_TOP - Z_BOT) / 2.0
R_BL = 4.5                 # bottom-left outside corner
F_NECK_L = 8.0             # concave blends of the outline
F_NECK_R = 8.0
F_LOW_L = 4.0
F_ARM = 2.2
Z_RK = -5.8                # below this height the right edge leans slightly inward
RK_ANG = 12.4              # (deg from vertical) before blending into the arm

# raised boss around the bearing bore: footprint B (defined at the chamfer-start plane Y=YC)
# extruded toward the front with a 45 deg draft, so its flanks continue the perimeter chamfer
BOSS_C = MAIN_C
BOSS_R0 = MAIN_R + 0.25   # main circle of the boss footprint at Y=YC
BOSS_TOP_C = (0.0, 8.0)    # footprint stretched toward the top hole ...
BOSS_TOP_R = 9.4
BOSS_BOT_X0 = X_LEFT       # ... and a block toward the bottom hole
BOSS_BOT_X1 = 13.0
BOSS_BOT_Z0 = -13.9
BOSS_BOT_Z1 = -3.0
BOSS_LR_P0 = (7.33, -13.6)  # straight lower-right flank of the boss
BOSS_LR_P1 = (11.67, -8.34)
BOSS_TRIM_C = (-2.68, 0.23)  # arc bounding the right-hand flank
BOSS_TRIM_R = 16.84
BOSS_TRIM_ZLOW = -8.5      # the arc only acts above this height
BOSS_FR = 1.5              # round between flank and top face

# holes
BIG_C = (0.0, 0.0)
BIG_R1 = 6.1               # front lip bore
BIG_R2 = 7.4               # back counterbore (bearing seat)
BIG_D2 = 4.5               # depth of back counterbore
BIG_CH = 1.0
BIG_CH_BACK = 0.4
TOPH_R = 2.85
BOT_C = (0.0, -15.7)
BOTH_R = 2.95
RH_C = (ARM_END_X, ARM_ZC)
RH_R = 2.82
H_CH = 0.7
H_CH_BACK = 0.5
SLOT_C = (12.85, ARM_ZC)
SLOT_L = 10.8
SLOT_W = 3.7
SLOT_CH = 0.45

# counterbores around top and bottom holes (cut into the boss down to the plate face)
CBR_TOP = 5.6
CBR_BOT = 5.6
CBR_CH = 0.9

# shallow notch on the right edge
NOTCH_Z = 0.5
NOTCH_R = 4.25             # radius of the notch
NOTCH_DEPTH = 0.75         # depth below the straight right edge
NOTCH_K = 0.0              # radius growth per mm toward the front (0 = straight)

# ---------------------------------------------------------------- 2D helpers


def unit(v):
    l = math.hypot(v[0], v[1])
    return (v[0] / l, v[1] / l)


def add(a, b, s=1.0):
    return (a[0] + s * b[0], a[1] + s * b[1])


def sub(a, b):
    return (a[0] - b[0], a[1] - b[1])


def circle_circle(c1, r1, c2, r2):
    dx, dz = c2[0] - c1[0], c2[1] - c1[1]
    d = math.hypot(dx, dz)
    a = (r1 * r1 - r2 * r2 + d * d) / (2 * d)
    h = math.sqrt(max(r1 * r1 - a * a, 0.0))
    ux, uz = dx / d, dz / d
    bx, bz = c1[0] + a * ux, c1[1] + a * uz
    return (bx - h * uz, bz + h * ux), (bx + h * uz, bz - h * ux)


def fillet_cc(c1, r1, c2, r2, f, pick):
    """concave blend of radius f between two convex arcs; returns (centre, tangent on 1, tangent on 2)"""
    cands = circle_circle(c1, r1 + f, c2, r2 + f)
    cf = pick(*cands)
    t1 = add(c1, unit(sub(cf, c1)), r1)
    t2 = add(c2, unit(sub(cf, c2)), r2)
    return cf, t1, t2


def arc_mid(c, r, p0, p1, ccw):
    a0 = math.atan2(p0[1] - c[1], p0[0] - c[0])
    a1 = math.atan2(p1[1] - c[1], p1[0] - c[0])
    if ccw:
        while a1 <= a0:
            a1 += 2 * math.pi
    else:
        while a1 >= a0:
            a1 -= 2 * math.pi
    am = 0.5 * (a0 + a1)
    return (c[0] + r * math.cos(am), c[1] + r * math.sin(am))


# ---------------------------------------------------------------- outline geometry
# right neck: upper-right arc -> top lobe
fNR, tRU, tTR = fillet_cc(RU_C, RU_R, TOP_C, TOP_R, F_NECK_R, lambda a, b: a if a[0] > b[0] else b)
# left neck: top lobe -> main arc
fNL, tTL, tML = fillet_cc(TOP_C, TOP_R, MAIN_C, MAIN_R, F_NECK_L, lambda a, b: a if a[0] < b[0] else b)
# lower left: main arc -> left edge (line X = X_LEFT, material on +X side)
_xc = X_LEFT - F_LOW_L
_zc = MAIN_C[1] - math.sqrt((MAIN_R + F_LOW_L) ** 2 - (_xc - MAIN_C[0]) ** 2)
fLL = (_xc, _zc)
tMLL = add(MAIN_C, unit(sub(fLL, MAIN_C)), MAIN_R)
tLL = (X_LEFT, _zc)
# arm / right edge blend (the right edge leans inward by RK_ANG below Z_RK)
_sb, _cb = math.sin(math.radians(RK_ANG)), math.cos(math.radians(RK_ANG))
_fz = Z_ARM_TOP + F_ARM
fAR = (X_RIGHT + (F_ARM + (_fz - Z_RK) * _sb) / _cb, _fz)
tAR_arm = (fAR[0], Z_ARM_TOP)                       # tangent on the arm top edge
tAR_edge = (fAR[0] - F_ARM * _cb, fAR[1] + F_ARM * _sb)  # tangent on the leaning edge


def outline_wp(wp):
    """draw the closed plate outline (counter-clockwise) on a workplane whose local x=X, y=Z"""
    p0 = (X_LEFT + R_BL, Z_BOT)
    w = wp.moveTo(*p0)
    w = w.lineTo(ARM_END_X, Z_BOT)
    w = w.threePointArc((ARM_END_X + ARM_R, ARM_ZC), (ARM_END_X, Z_ARM_TOP))
    w = w.lineTo(*tAR_arm)
    w = w.threePointArc(arc_mid(fAR, F_ARM, tAR_arm, tAR_edge, False), tAR_edge)
    w = w.lineTo(X_RIGHT, Z_RK)
    w = w.lineTo(X_RIGHT, RU_C[1])
    w = w.threePointArc(arc_mid(RU_C, RU_R, (X_RIGHT, RU_C[1]), tRU, True), tRU)
    w = w.threePointArc(arc_mid(fNR, F_NECK_R, tRU, tTR, False), tTR)
    w = w.threePointArc(arc_mid(TOP_C, TOP_R, tTR, tTL, True), tTL)
    w = w.threePointArc(arc_mid(fNL, F_NECK_L, tTL, tML, False), tML)
    w = w.threePointArc(arc_mid(MAIN_C, MAIN_R, tML, tMLL, True), tMLL)
    w = w.threePointArc(arc_mid(fLL, F_LOW_L, tMLL, tLL, False), tLL)
    w = w.lineTo(X_LEFT, Z_BOT + R_BL)
    w = w.threePointArc(arc_mid((X_LEFT + R_BL, Z_BOT + R_BL), R_BL, (X_LEFT, Z_BOT + R_BL), p0, True), p0)
    return w.close()


def outline(d, y0=0.0):
    """plate outline as a straight prism from Y=-y0 to Y=-(y0+d)"""
    return outline_wp(cq.Workplane("XZ").workplane(offset=y0)).extrude(d)


# ---------------------------------------------------------------- 3D helpers


def rev_cutter(c, profile):
    """solid of revolution about an axis parallel to Y through c=(X,Z); profile: closed list of (r, y)"""
    pts = [cq.Vector(c[0] + r, y, c[1]) for (r, y) in profile]
    w = cq.Wire.makePolygon(pts, close=True)
    f = cq.Face.makeFromWires(w)
    sol = cq.Solid.revolve(f, 360.0, cq.Vector(c[0], 0, c[1]), cq.Vector(c[0], 1, c[1]))
    return cq.Workplane("XY").add(sol)


def chamfered_hole(c, r, ch, y_front, ch_back=0.0, extra=1.0):
    """through hole of radius r with 45 deg chamfers: ch at the front face y_front, ch_back at the back face Y=0"""
    prof = [
        (0.0, extra),
        (r + ch_back + extra, extra),
        (r, -ch_back),
        (r, y_front + ch),
        (r + ch + extra, y_front - extra),
        (0.0, y_front - extra),
    ]
    return rev_cutter(c, prof)


# ---------------------------------------------------------------- plate
plate = outline(T).faces("<Y").edges().chamfer(C1)

# ---------------------------------------------------------------- boss
def disc2d(c, r):
    return cq.Face.makeFromWires(cq.Wire.makeCircle(r, cq.Vector(c[0], c[1], 0), cq.Vector(0, 0, 1)))


def poly2d(pts):
    return cq.Face.makeFromWires(cq.Wire.makePolygon([cq.Vector(x, y, 0) for (x, y) in pts], close=True))


def rect2d(x0, x1, y0, y1):
    return poly2d([(x0, y0), (x1, y0), (x1, y1), (x0, y1)])


# footprint B of the boss at the chamfer-start plane (2D, local x = X, local y = Z)
_lx = BOSS_LR_P1[0] - BOSS_LR_P0[0]
_lz = BOSS_LR_P1[1] - BOSS_LR_P0[1]
_ll = math.hypot(_lx, _lz)
_ux, _uz = _lx / _ll, _lz / _ll
_nx, _nz = -_uz, _ux                       # normal pointing into the boss (up-left)
_p0 = (BOSS_LR_P0[0] - 40 * _ux, BOSS_LR_P0[1] - 40 * _uz)
_p1 = (BOSS_LR_P0[0] + 40 * _ux, BOSS_LR_P0[1] + 40 * _uz)
half_lr = poly2d([_p0, _p1, (_p1[0] + 80 * _nx, _p1[1] + 80 * _nz), (_p0[0] + 80 * _nx, _p0[1] + 80 * _nz)])
b2d = disc2d(BOSS_C, BOSS_R0).fuse(disc2d(BOSS_TOP_C, BOSS_TOP_R))
b2d = b2d.fuse(rect2d(BOSS_BOT_X0, BOSS_BOT_X1, BOSS_BOT_Z0, BOSS_BOT_Z1))
b2d = b2d.intersect(half_lr)
b2d = b2d.intersect(disc2d(BOSS_TRIM_C, BOSS_TRIM_R).fuse(rect2d(-40, 40, -40, BOSS_TRIM_ZLOW)))
b2d = b2d.clean()
boss_sk = cq.Sketch().face(b2d.Faces()[0])
boss = cq.Workplane("XZ").workplane(offset=-YC).placeSketch(boss_sk).extrude(TB + YC, taper=45)
boss = boss.faces("<Y").edges().fillet(BOSS_FR)
boss = boss.intersect(outline(TB))
body = plate.union(boss)

# counterbores around the top and bottom holes (down to the plate face)
for (c, rc) in ((TOP_C, CBR_TOP), (BOT_C, CBR_BOT)):
    prof = [
        (0.0, -T),
        (rc, -T),
        (rc, -TB + CBR_CH),
        (rc + CBR_CH + 2.0, -TB - 2.0),
        (0.0, -TB - 2.0),
    ]
    body = body.cut(rev_cutter(c, prof))

# ---------------------------------------------------------------- holes
body = body.cut(chamfered_hole(TOP_C, TOPH_R, H_CH, -T, H_CH_BACK))
body = body.cut(chamfered_hole(BOT_C, BOTH_R, H_CH, -T, H_CH_BACK))
body = body.cut(chamfered_hole(RH_C, RH_R, H_CH, -T, H_CH_BACK))
body = body.cut(chamfered_hole(BIG_C, BIG_R1, BIG_CH, -TB))
# bearing seat from the back, with a small lead-in chamfer
body = body.cut(rev_cutter(BIG_C, [
    (0.0, 1.0),
    (BIG_R2 + BIG_CH_BACK + 1.0, 1.0),
    (BIG_R2, -BIG_CH_BACK),
    (BIG_R2, -BIG_D2),
    (0.0, -BIG_D2),
]))

# slot with a small front chamfer
slot = (cq.Workplane("XZ").workplane(offset=-1.0).center(*SLOT_C)
        .slot2D(SLOT_L, SLOT_W).extrude(T + 2.0))
body = body.cut(slot)
slot_ch = (cq.Workplane("XZ").workplane(offset=T - SLOT_CH).center(*SLOT_C)
           .slot2D(SLOT_L, SLOT_W).extrude(SLOT_CH + 1.0, taper=-45))
body = body.cut(slot_ch)

# shallow notch in the right edge
notch_c = (X_RIGHT + NOTCH_R - NOTCH_DEPTH, NOTCH_Z)
notch = rev_cutter(notch_c, [
    (0.0, 1.0),
    (NOTCH_R - NOTCH_K * 1.0, 1.0),
    (NOTCH_R + NOTCH_K * (TB + 1.0), -TB - 1.0),
    (0.0, -TB - 1.0),
])
body = body.cut(notch)

result = body.clean()
